import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 60.0            # plate length (X)
D = 20.0            # plate depth (Y)
T = 5.2             # plate thickness (Z)
R_EDGE = 0.8        # outer edge fillet (all outer edges)

RIM = 3.2           # rim width around the recessed panel
POCKET_DEPTH = 1.9  # depth of the recessed panel
POCKET_CORNER = 0.6 # plan-view corner radius of the panel
POCKET_FLOOR_R = 0.8  # fillet between panel floor and walls

RING_OD = 13.3      # hanging ring outer diameter
RING_ID = 9.5       # hanging ring hole diameter
RING_T = 3.35       # hanging ring thickness (flush with plate bottom)
RING_X = 0.67       # ring centre offset along X (centre lies on back edge)

TEXT = "Clase de Antonia"
TEXT_W = 37.45      # overall text length
TEXT_H = 9.9        # overall text height (ascender height)
TEXT_DX = -0.12     # text centre offset along X
TEXT_DY = 0.2       # text centre offset towards the back (+Y)
TEXT_TOP = T        # lettering top flush with the rim

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- plate ----------------
plate = (
    cq.Workplane("XY")
    .box(W, D, T, centered=(True, True, False))
    .edges()
    .fillet(R_EDGE)
)

# ---------------- hanging ring (added after the plate is rounded) -------
ring = (
    cq.Workplane("XY")
    .center(RING_X, D / 2.0)
    .circle(RING_OD / 2.0)
    .circle(RING_ID / 2.0)
    .extrude(RING_T)
)
body = plate.union(ring)

# ---------------- recessed panel ----------------
floor_z = T - POCKET_DEPTH
pw, pd = W - 2 * RIM, D - 2 * RIM
pocket = (
    cq.Workplane("XY", origin=(0, 0, floor_z))
    .rect(pw, pd)
    .extrude(POCKET_DEPTH + 1.0)
    .edges("|Z")
    .fillet(POCKET_CORNER)
    .faces("<Z")
    .edges()
    .fillet(POCKET_FLOOR_R)
)
body = body.cut(pocket)

# ---------------- raised lettering ----------------
SINK = 0.2                                   # letters sink into the floor
txt_h = TEXT_TOP - floor_z + SINK


def make_text(h):
    # condensed sans-serif lettering; fall back gracefully if a font is absent
    for kw in ({"font": "DejaVu Sans", "kind": "bold"}, {"kind": "bold"}, {}):
        try:
            w = cq.Workplane("XY").text(
                TEXT, 10.0, h, halign="center", valign="center", **kw
            )
            v = w.val()
            if v.isValid() and v.Volume() > 0:
                return v
        except Exception:
            pass
    return None


shp = make_text(txt_h)
if shp is not None:
    bb = shp.BoundingBox()
    sx = TEXT_W / (bb.xmax - bb.xmin)        # condense the lettering
    sy = TEXT_H / (bb.ymax - bb.ymin)
    cx = (bb.xmax + bb.xmin) / 2.0
    cy = (bb.ymax + bb.ymin) / 2.0
    m = cq.Matrix(
        [
            [sx, 0.0, 0.0, -cx * sx + TEXT_DX],
            [0.0, sy, 0.0, -cy * sy + TEXT_DY],
            [0.0, 0.0, 1.0, floor_z - SINK],
        ]
    )
    letters = shp.transformGeometry(m)
    result = body.union(cq.Workplane("XY").add(letters))
else:
    result = body
